import math
import cadquery as cq

# Open-top electronics enclosure with hanging corner screw posts, PCB
# standoffs, a slot and a round jack hole in the back wall and a cable
# notch in the front wall, plus its flat screw-on lid shown lifted and
# moved aside (two separate solids).

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
# enclosure body
L = 113.0          # outer length (X)
W = 80.0           # outer width (Y)
H = 32.0           # outer height (Z)
T = 2.0            # wall thickness
TF = 4.0           # floor thickness
EDGE_R = 0.5       # vertical outer edge fillet
BASE_H = 1.5       # bottom plate (kept as a separate face band)

# corner screw posts (hang from the rim)
P = 6.0            # post size (square, measured from inner wall)
POST_Z_WALL = 15.5  # height of the post underside where it meets a wall
POST_K = 0.65       # rise of the underside per mm away from each wall
POST_HOLE_D = 2.2
POST_HOLE_INSET = 4.6   # hole centre from the outer faces
POST_HOLE_DEPTH = 10.0
# support rib continuing the +X face of the back-left post downwards
RIB_T = 1.2
RIB_Z_IN, RIB_Z_WALL = 15.7, 11.5   # underside height at post edge / at wall

# PCB standoffs on the floor
SO_X = (-48.2, 41.2)
SO_Y = 32.6
SO_D1, SO_H1 = 5.8, 3.5    # base
SO_D2, SO_H2 = 3.4, 3.8    # pin

# notch in the top of the front wall
NOTCH_X0, NOTCH_X1 = -44.6, -16.8
NOTCH_DEPTH = 3.8
NOTCH_R = 0.5

# back wall openings
SLOT_X0, SLOT_X1 = -44.4, -12.3
SLOT_Z0, SLOT_Z1 = 10.5, 13.5
JACK_X, JACK_Z, JACK_D = 31.0, 13.5, 7.8

# lid (shown lifted and moved aside)
LID_L, LID_W, LID_T = 113.0, 80.0, 2.2
LID_POS = (125.3, -62.5, 42.6)      # centre X, centre Y, bottom Z
LID_HOLE_D = 2.9
LID_HOLE_INSET = 4.6
GROOVE_W = 0.7       # perimeter groove width
GROOVE_D = 0.8       # perimeter groove depth
DIAG_W0 = 0.9        # diagonal V-groove width at its narrow end
DIAG_W1 = 1.8        # diagonal V-groove width at its wide end
DIAG_K = 1.4         # depth / half-width of the V-groove

# ---------------- enclosure body ----------------
body = (cq.Workplane("XY").workplane(offset=BASE_H)
        .rect(L, W).extrude(H - BASE_H)
        .edges("|Z").fillet(EDGE_R))

cavity = (cq.Workplane("XY").workplane(offset=TF)
          .rect(L - 2 * T, W - 2 * T).extrude(H))
body = body.cut(cavity)

# corner posts: square prism hanging from the rim; the underside is hip
# shaped (z = z0 + k * min(dist to X wall, dist to Y wall)) so it merges
# into both walls without overhang
xi = L / 2 - T
yi = W / 2 - T


def corner_post():
    z0 = POST_Z_WALL
    z1 = POST_Z_WALL + POST_K * P
    # wedge whose underside rises away from the X wall
    wa = (cq.Workplane("XZ")
          .polyline([(xi, z0), (xi - P, z1), (xi - P, H), (xi, H)])
          .close().extrude(-P).translate((0, yi - P, 0)))
    # wedge whose underside rises away from the Y wall
    wb = (cq.Workplane("YZ")
          .polyline([(yi, z0), (yi - P, z1), (yi - P, H), (yi, H)])
          .close().extrude(P).translate((xi - P, 0, 0)))
    return wa.union(wb)


post = corner_post()
posts = post.union(post.mirror("YZ"))
posts = posts.union(posts.mirror("XZ"))
body = body.union(posts)

# rib under the (-X,+Y) post, in the plane of its +X face
rib_x = -xi + P
rib = (cq.Workplane("YZ", origin=(rib_x - RIB_T, 0, 0))
       .polyline([(yi - P, RIB_Z_IN), (yi, RIB_Z_WALL), (yi, H - 4), (yi - P, H - 4)])
       .close().extrude(RIB_T))
body = body.union(rib)

# screw holes in the posts
body = body.cut(
    cq.Workplane("XY").workplane(offset=H - POST_HOLE_DEPTH)
    .pushPoints([(sx * (L / 2 - POST_HOLE_INSET), sy * (W / 2 - POST_HOLE_INSET))
                 for sx in (-1, 1) for sy in (-1, 1)])
    .circle(POST_HOLE_D / 2).extrude(POST_HOLE_DEPTH + 1))

# standoffs
pts = [(x, sy * SO_Y) for x in SO_X for sy in (-1, 1)]
so = (cq.Workplane("XY").workplane(offset=TF - 0.1).pushPoints(pts)
      .circle(SO_D1 / 2).extrude(SO_H1 + 0.1)
      .faces(">Z").workplane().pushPoints(pts)
      .circle(SO_D2 / 2).extrude(SO_H2))
body = body.union(so)

# front wall notch (rounded bottom corners)
nw = NOTCH_X1 - NOTCH_X0
notch = (cq.Workplane("XZ", origin=(0, -W / 2 + T + 1, 0))
         .center((NOTCH_X0 + NOTCH_X1) / 2, H - NOTCH_DEPTH + (NOTCH_DEPTH + 2) / 2)
         .rect(nw, NOTCH_DEPTH + 2).extrude(T + 2))
notch = notch.edges("|Y").edges("<Z").fillet(NOTCH_R)
body = body.cut(notch)

# back wall slot
sw = SLOT_X1 - SLOT_X0
slot = (cq.Workplane("XZ", origin=(0, W / 2 + 1, 0))
        .center((SLOT_X0 + SLOT_X1) / 2, (SLOT_Z0 + SLOT_Z1) / 2)
        .rect(sw, SLOT_Z1 - SLOT_Z0).extrude(T + 2))
body = body.cut(slot)

# back wall round hole
jack = (cq.Workplane("XZ", origin=(0, W / 2 + 1, 0))
        .center(JACK_X, JACK_Z).circle(JACK_D / 2).extrude(T + 2))
body = body.cut(jack)

# ---------------- lid ----------------
lid = cq.Workplane("XY").box(LID_L, LID_W, LID_T, centered=(True, True, False))
hx = LID_L / 2 - LID_HOLE_INSET
hy = LID_W / 2 - LID_HOLE_INSET


def ring_groove(z_face, up):
    """rectangular groove running through the four hole centres"""
    d = GROOVE_D
    zb = z_face - d if up else z_face - 0.01
    return (cq.Workplane("XY").workplane(offset=zb)
            .rect(2 * hx + GROOVE_W, 2 * hy + GROOVE_W)
            .rect(2 * hx - GROOVE_W, 2 * hy - GROOVE_W)
            .extrude(d + 0.01))


def v_groove(p0, p1, w0, w1, z_face, up):
    """tapered V-groove from p0 (width w0) to p1 (width w1) in a face"""
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    ln = math.hypot(dx, dy)
    nx, ny = -dy / ln, dx / ln
    into = -1.0 if up else 1.0          # direction into the material
    eps = 0.05

    def section(p, w):
        a = w / 2
        return cq.Wire.makePolygon([
            cq.Vector(p[0] + nx * (a + eps), p[1] + ny * (a + eps), z_face - into * eps * DIAG_K),
            cq.Vector(p[0] - nx * (a + eps), p[1] - ny * (a + eps), z_face - into * eps * DIAG_K),
            cq.Vector(p[0], p[1], z_face + into * a * DIAG_K),
        ], close=True)

    return cq.Solid.makeLoft([section(p0, w0), section(p1, w1)], ruled=True)


# top: perimeter groove + diagonal from the (-X,+Y) hole to the (+X,-Y) hole
lid = lid.cut(ring_groove(LID_T, True))
lid = lid.cut(v_groove((-hx, hy), (hx, -hy), DIAG_W0, DIAG_W1, LID_T, True))
# underside: perimeter groove + the other diagonal
lid = lid.cut(ring_groove(0.0, False))
lid = lid.cut(v_groove((-hx, -hy), (hx, hy), GROOVE_W, GROOVE_W, 0.0, False))
lid = lid.cut(
    cq.Workplane("XY").pushPoints([(sx * hx, sy * hy) for sx in (-1, 1) for sy in (-1, 1)])
    .circle(LID_HOLE_D / 2).extrude(LID_T))
lid = lid.translate(LID_POS)

# bottom plate joined without merging the coplanar side faces
base = (cq.Workplane("XY").rect(L, W).extrude(BASE_H)
        .edges("|Z").fillet(EDGE_R))
body = body.union(base, clean=False)

result = body.union(lid, clean=False)
